import math
import cadquery as cq

# =====================================================================
#  Conical adapter / hood: a revolved body with a steep nose cone at the
#  small (front, -Y) end, a shallow main cone, a thick-walled cylindrical
#  bore, a counterbore at the large (back, +Y) end with three axial screw
#  holes, one window through the +X wall and a half-round key inside.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
D_LARGE = 100.0      # outer diameter at the large (back, +Y) end
D_SMALL = 75.9       # outer diameter at the small (front, -Y) end
D_KNEE = 86.8        # outer diameter at the knee between the steep nose and the main cone
L_TOTAL = 48.8       # overall axial length
L_NOSE = 11.8        # axial length of the steep nose cone
D_BORE_SMALL = 73.0  # bore diameter at the small end (thin nose wall)
D_BORE = 84.0        # main cylindrical bore diameter
D_CBORE = 96.6       # counterbore diameter at the large end
CBORE_DEPTH = 3.5    # counterbore depth from the large end face

# three axial screw holes in the counterbore shoulder
HOLE_PCD = 89.0
HOLE_D = 3.4
HOLE_DEPTH = 6.0
HOLE_ANGLES = (0.0, 120.0, 240.0)   # measured from +X toward +Z

# rounded-rectangle window through the +X side wall
WIN_W = 6.6          # along the axis (Y)
WIN_H = 12.1         # along Z
WIN_R = 1.0          # corner radius
WIN_TILT = 15.0      # cut direction tilted up (outward) from the X axis, deg
WIN_Y = 2.6          # window centre, axial position (0 = mid length)
WIN_Z = 4.5          # window centre height (on the outer surface)

# half-round key on the inside of the nose, +X side
KEY_R = 4.2
KEY_Y_FACE = -13.6   # position of its flat end face (faces the large end)
KEY_Z = 1.5
KEY_SLOPE = 0.0      # key axis leans toward the part axis by this slope toward the small end
KEY_LEN = 7.9        # key length along its axis
KEY_OFF = 0.1        # key axis offset outward from the nose bore surface

SEAM_ANGLE = 135.0   # rotate the revolve seam to the lower back side

VIEW = {"azimuth": 45, "elevation": 26}   # default camera

# ---------------- derived values ----------------
R0, R1, R2 = D_SMALL / 2, D_KNEE / 2, D_LARGE / 2
Y0 = -L_TOTAL / 2
Y1 = Y0 + L_NOSE
Y2 = L_TOTAL / 2
slope_nose = (R1 - R0) / (Y1 - Y0)
RI0 = D_BORE_SMALL / 2
RB = D_BORE / 2
RCB = D_CBORE / 2
Y_IK = Y0 + (RB - RI0) / slope_nose      # inner knee: nose bore meets main bore
Y_SH = Y2 - CBORE_DEPTH                  # counterbore floor (shoulder)


# ---------------- body of revolution (profile in the X-Y plane, revolved about Y) -------------
profile = [
    (R0, Y0),          # small end, outside
    (R1, Y1),          # outer knee
    (R2, Y2),          # large end, outside
    (RCB, Y2),         # large end face -> counterbore
    (RCB, Y_SH),       # counterbore floor (shoulder)
    (RB, Y_SH),        # shoulder inner edge
    (RB, Y_IK),        # main bore -> inner knee
    (RI0, Y0),         # nose bore to the small end
]
body = (
    cq.Workplane("XY")
    .polyline(profile)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 1, 0), SEAM_ANGLE)   # put the revolve seam on the lower back side
)

# ---------------- axial blind holes in the shoulder ----------------
hole_r = HOLE_PCD / 2
for a in HOLE_ANGLES:
    ar = math.radians(a)
    x, z = hole_r * math.cos(ar), hole_r * math.sin(ar)
    h = (
        cq.Workplane("XZ", origin=(0, Y_SH + 0.01, 0))   # XZ normal is -Y: drills toward the small end
        .center(x, z)
        .circle(HOLE_D / 2)
        .extrude(HOLE_DEPTH)
    )
    body = body.cut(h)

# ---------------- window through the +X wall ----------------
# rounded-rectangle prism, its axis tilted WIN_TILT degrees upward (outward), centred on the outer surface
r_win = R1 + (R2 - R1) * (WIN_Y - Y1) / (Y2 - Y1)      # outer radius at the window
t = math.radians(WIN_TILT)
wdir = cq.Vector(math.cos(t), 0, math.sin(t))
wplane = cq.Plane(
    origin=cq.Vector(r_win, WIN_Y, WIN_Z) - wdir * 15.0,
    xDir=cq.Vector(0, 1, 0),
    normal=wdir,
)
win = cq.Workplane(wplane).sketch().rect(WIN_W, WIN_H).vertices().fillet(WIN_R).finalize().extrude(30)
body = body.cut(win)

# ---------------- half-round key inside the nose ----------------
r_wall = RI0 + slope_nose * (KEY_Y_FACE - Y0)      # nose bore radius at the key face
kdir = cq.Vector(-KEY_SLOPE, -1.0, 0.0).normalized()
kplane = cq.Plane(
    origin=cq.Vector(r_wall + KEY_OFF, KEY_Y_FACE, KEY_Z),
    xDir=cq.Vector(0, 0, 1),
    normal=kdir,
)
key = cq.Workplane(kplane).circle(KEY_R).extrude(KEY_LEN)
# keep the key inside the nose wall: clip it to the outer envelope shrunk by KEY_SKIN
KEY_SKIN = 0.6
envelope = (
    cq.Workplane("XY")
    .polyline([(0, Y0), (R0 - KEY_SKIN, Y0), (R1 - KEY_SKIN, Y1), (R2 - KEY_SKIN, Y2), (0, Y2)])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
key = key.intersect(envelope)
body = body.union(key)

result = body
